import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 40.0            # pipe outer diameter
WALL = 3.3          # pipe wall thickness
L1 = 135.0          # straight run from the open -Y end to the start of the bend
R_BEND = 37.0       # bend centre-line radius
BEND_DEG = 50.0     # bend angle (towards +X)
L2 = 26.5           # straight run after the bend

PORT_YC = 41.6      # Y position of the side ports centre (from the -Y end)

# +X side : stadium boss + flange with two ears, blind stadium pocket
BOX_L, BOX_H = 78.0, 25.0       # boss stadium (along Y, along Z)
FL_L, FL_H = 82.0, 30.0         # flange stadium
FL_T = 5.6                      # flange thickness
FL_X = 45.5                     # flange outer face X position
FL_ZC = 0.25                    # flange / boss centre height above pipe axis
PORT_TILT = 2.0                 # +X port axis tilted up (deg, about the pipe axis)
EAR_R = 9.5                     # ear radius
EAR_IN = 0.5                    # ear centre inset from the flange edge
HOLE_Z = 19.6                   # ear hole offset from flange centre (Z)
EAR_HOLE_D = 6.8                # ear hole diameter
EAR_FIL = 1.0                   # ear-to-flange blend radius
PASS_L, PASS_H = 68.0, 17.0     # stadium pocket in the boss/flange

# -X side : thin stadium spigot, open into the pipe
SP_L, SP_H = 75.0, 23.5         # spigot outer stadium
SP_X = 29.0                     # spigot reach from the pipe axis (-X)
SP_WALL = 3.25                  # spigot wall
SP_CH = 0.8                     # chamfer at the spigot mouth

# small slot near the bent end
SLOT_L, SLOT_W = 14.0, 4.0
SLOT_BACK = 21.0                # distance back from the end face along axis
SLOT_ANG = 45.0                 # angle above the equator on the outer side
SLOT_DEPTH = 2.0                # blind recess depth

SEAM_ANG = 45.0                 # where the sweep seam of the pipe lies

ro = D / 2.0
ri = ro - WALL
th = math.radians(BEND_DEG)


def pipe_path(ext0=0.0, ext1=0.0):
    """Centre line: straight run, circular bend (towards +X), straight run."""
    V = cq.Vector
    p0 = V(0, -ext0, 0)
    p1 = V(0, L1, 0)
    c = V(R_BEND, L1, 0)
    pm = c + V(-R_BEND * math.cos(th / 2), R_BEND * math.sin(th / 2), 0)
    p2 = c + V(-R_BEND * math.cos(th), R_BEND * math.sin(th), 0)
    d = V(math.sin(th), math.cos(th), 0)
    p3 = p2 + d * (L2 + ext1)
    wire = cq.Wire.assembleEdges([
        cq.Edge.makeLine(p0, p1),
        cq.Edge.makeThreePointArc(p1, pm, p2),
        cq.Edge.makeLine(p2, p3),
    ])
    return wire, p2, p3, d


def swept_rod(radius, ext0=0.0, ext1=0.0):
    """Round bar swept along the centre line (cylinder - torus - cylinder)."""
    path, _, _, _ = pipe_path(ext0, ext1)
    sa = math.radians(SEAM_ANG)        # put the profile seam on the outer/upper side
    pl = cq.Plane(origin=(0, -ext0, 0), xDir=(-math.cos(sa), 0, math.sin(sa)),
                  normal=(0, 1, 0))
    return cq.Workplane(pl).circle(radius).sweep(cq.Workplane().add(path),
                                                 transition="round")


def stadium_x(length, height, x0, depth, yc=PORT_YC, zc=0.0):
    """Stadium (long along Y) drawn in the plane X = x0 and extruded by depth
    along X (negative depth goes towards -X)."""
    return (cq.Workplane("YZ", origin=(x0, 0, 0)).center(yc, zc)
            .slot2D(length, height).extrude(depth))


# ---------------- main pipe (solid for now) ----------------
pipe_solid = swept_rod(ro)
body = pipe_solid

# ---------------- +X boss and flange (built on +X, then tilted) ----------------
fl_in = FL_X - FL_T


def tilt(wp):
    """Tilt a +X port feature upward about the pipe axis (Y axis)."""
    return wp.rotate((0, 0, 0), (0, 1, 0), -PORT_TILT)


boss = stadium_x(BOX_L, BOX_H, -2.0, fl_in + 2.0, zc=FL_ZC)
flange = stadium_x(FL_L, FL_H, fl_in, FL_T, zc=FL_ZC)
ear_pts = [(PORT_YC, FL_ZC + FL_H / 2 - EAR_IN), (PORT_YC, FL_ZC - FL_H / 2 + EAR_IN)]
ears = (cq.Workplane("YZ", origin=(fl_in, 0, 0)).pushPoints(ear_pts)
        .circle(EAR_R).extrude(FL_T))
flange = flange.union(ears)
# blend the ears into the flange outline (edges parallel to X at the junctions)
_jy = math.sqrt(EAR_R ** 2 - EAR_IN ** 2)
junctions = [(PORT_YC + sy * _jy, FL_ZC + sz * FL_H / 2)
             for sy in (1, -1) for sz in (1, -1)]


def _is_junction(e):
    c = e.Center()
    return any(abs(c.y - jy) < 0.3 and abs(c.z - jz) < 0.3 for jy, jz in junctions)


sel = [e for e in flange.edges("|X").vals() if _is_junction(e)]
if sel and EAR_FIL > 0:
    flange = flange.newObject(sel).fillet(EAR_FIL)
body = body.union(tilt(boss.union(flange)))

# ---------------- -X spigot ----------------
body = body.union(stadium_x(SP_L, SP_H, 0.0, -SP_X))

# ---------------- bores, pocket and passages ----------------
body = body.cut(swept_rod(ri, 1.0, 1.0))
# blind pocket in the +X boss: stops on the outside of the pipe wall
pocket = tilt(stadium_x(PASS_L, PASS_H, 0.0, FL_X + 2, zc=FL_ZC)).cut(pipe_solid)
body = body.cut(pocket)
# open passage through the -X spigot and the pipe wall into the bore
body = body.cut(stadium_x(SP_L - 2 * SP_WALL, SP_H - 2 * SP_WALL, 0.0, -SP_X - 2))
# mouth chamfer
mouth = (cq.Workplane("YZ", origin=(-SP_X, 0, 0)).center(PORT_YC, 0)
         .slot2D(SP_L - 2 * SP_WALL + 2 * SP_CH, SP_H - 2 * SP_WALL + 2 * SP_CH)
         .workplane(offset=SP_CH)
         .slot2D(SP_L - 2 * SP_WALL, SP_H - 2 * SP_WALL)
         .loft(ruled=True))
body = body.cut(mouth)

holes = (cq.Workplane("YZ", origin=(fl_in - 1, 0, 0))
         .pushPoints([(PORT_YC, FL_ZC + HOLE_Z), (PORT_YC, FL_ZC - HOLE_Z)])
         .circle(EAR_HOLE_D / 2).extrude(FL_T + 2))
body = body.cut(tilt(holes))

# ---------------- small slot near the bent end ----------------
_, p2, p3, dvec = pipe_path()
out_n = cq.Vector(-math.cos(th), math.sin(th), 0)       # outer side of the bend
a = math.radians(SLOT_ANG)
radial = out_n * math.cos(a) + cq.Vector(0, 0, 1) * math.sin(a)
sc = p3 - dvec * SLOT_BACK
slot_plane = cq.Plane(origin=sc + radial * (ro - SLOT_DEPTH), xDir=dvec, normal=radial)
slot = cq.Workplane(slot_plane).rect(SLOT_L, SLOT_W).extrude(SLOT_DEPTH + 3)
body = body.cut(slot)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
